import cadquery as cq

# =====================================================================
#  Housing block: open-bottom cavity, top cable bridge, side ports
# =====================================================================

# ---------------- overall block (mm) ----------------
W = 100.0      # length along X
D = 80.0       # depth along Y
H = 55.0       # height along Z

# ---------------- top: shelves, corner posts and bridge plate ----------------
POST = 5.5     # square corner post
SHELF_W = 18.5 # Y-width of the front and back shelves
SHELF_D = 7.5  # shelf depth below the top face
SHELF_R = 6.5  # concave fillet between posts and shelf floor (mitred)
LIP_T = 2.0    # thickness of the bridge plate over the through slot
RIB_W = 5.5    # centre rib supporting the bridge plate

# ---------------- housing cavity (open at the bottom) ----------------
WALL_XM = 7.0  # -X wall
WALL_XP = 6.0  # +X wall
WALL_YM = 6.0  # -Y (front) wall
WALL_YP = 5.0  # +Y (back) wall
CAV_H = 43.7   # ceiling height
CAV_R = 7.0    # vertical corner radius of the cavity

# bottom sealing face: seal groove between an outer lip and an inner land
GRV_O = 1.0    # groove outer offset from the outside faces
GRV_I = 3.5    # groove inner offset from the outside faces
GRV_D = 1.0    # groove depth
BORDER_RC = 12.0  # corner radius of the bottom outlines measured at the outside faces
EDGE_CH = 1.2  # chamfer round the cavity opening

# pad on the inside of the -X wall behind the two back ports
PAD_T = 2.0
PAD_FR = 1.2

# small chamfered hole in the ceiling
CH_X, CH_Y = 33.5, 58.9
CH_D = 2.5
CH_CSK = 5.0
CH_DEPTH = 3.0

# ---------------- ports ----------------
BIG_T = 16.3   # threaded port (modelled as a plain bore)
BIG_P = 14.3   # plain port
PORT_Y = 15.0  # port axes distance from the front / back faces
PORT_ZP = 36.5 # port height on the +X face
PORT_ZM = 33.4 # port height on the -X face
LOW_Z = 12.6   # lower (plain) port on the -X face

# small tapped holes: same triangular pattern centred on every side face
SM_D = 3.3
SM_ZH = 32.5
SM_ZL = 7.5
SM_DX = 10.75
SM_BLIND = 4.5

eps = 1.0

# cavity extents
CX0, CX1 = WALL_XM, W - WALL_XP
CY0, CY1 = WALL_YM, D - WALL_YP


def rrect_prism(x0, x1, y0, y1, z0, z1, r):
    """Axis-aligned prism with rounded vertical edges."""
    return (
        cq.Workplane("XY")
        .rect(x1 - x0, y1 - y0)
        .extrude(z1 - z0)
        .edges("|Z")
        .fillet(r)
        .translate(((x0 + x1) / 2, (y0 + y1) / 2, z0))
    )


# =====================================================================
body = cq.Workplane("XY").box(W, D, H, centered=False)


# ---------------- top shelves with corner posts (mitred fillets) ----------------
def shelf_cut(y0, y1, post_low):
    """Material removed for one shelf band y0..y1: union of an XZ-profile
    slot (running along Y) and a YZ-profile slot (running along X), each
    filleted next to the posts, which leaves mitred fillets round the posts."""
    ys = y0 - eps if post_low else y0          # open towards the outside face only
    cut_x = (
        cq.Workplane("XY")
        .box(W - 2 * POST, (y1 - y0) + eps, SHELF_D + eps, centered=False)
        .translate((POST, ys, H - SHELF_D))
        .edges("|Y and <Z")
        .fillet(SHELF_R)
    )
    ya, yb = (y0 + POST, y1) if post_low else (y0, y1 - POST)
    cut_y = cq.Workplane("XY").box(W + 2 * eps, yb - ya, SHELF_D + eps, centered=False).translate(
        (-eps, ya, H - SHELF_D)
    )
    cut_y = cut_y.edges("|X and <Z and <Y" if post_low else "|X and <Z and >Y").fillet(SHELF_R)
    return cut_x.union(cut_y)


body = body.cut(shelf_cut(0.0, SHELF_W, True))
body = body.cut(shelf_cut(D - SHELF_W, D, False))

# through slot (along Y) under the bridge plate, split by a centre rib
slot = cq.Workplane("XY").box(W - 2 * POST, D - 2 * SHELF_W + 2 * eps, SHELF_D - LIP_T, centered=False).translate(
    (POST, SHELF_W - eps, H - SHELF_D)
)
rib = cq.Workplane("XY").box(RIB_W, D, H, centered=False).translate((W / 2 - RIB_W / 2, 0, 0))
body = body.cut(slot.cut(rib))

# ---------------- hollow housing, open at the bottom ----------------
def cavity_outline(grow=0.0):
    """Closed 2D outline of the cavity grown outward by `grow`: three rounded
    corners, the (-X,+Y) corner left square (the port pad fills it)."""
    x0, x1, y0, y1 = CX0 - grow, CX1 + grow, CY0 - grow, CY1 + grow
    r = CAV_R + grow
    k = 1.0 - 2 ** -0.5
    return (
        cq.Workplane("XY")
        .moveTo(x0, y1)
        .lineTo(x0, y0 + r)
        .threePointArc((x0 + r * k, y0 + r * k), (x0 + r, y0))
        .lineTo(x1 - r, y0)
        .threePointArc((x1 - r * k, y0 + r * k), (x1, y0 + r))
        .lineTo(x1, y1 - r)
        .threePointArc((x1 - r * k, y1 - r * k), (x1 - r, y1))
        .close()
    )


body = body.cut(cavity_outline().extrude(CAV_H + eps).translate((0, 0, -eps)))

# chamfer round the cavity opening (45 deg tapered cut)
body = body.cut(cavity_outline(EDGE_CH).extrude(EDGE_CH, taper=45).translate((0, 0, -0.001)))

# seal groove in the bottom face, concentric with the cavity corners
def rrect_offset(o, z0, z1):
    return rrect_prism(o, W - o, o, D - o, z0, z1, BORDER_RC - o)


body = body.cut(rrect_offset(GRV_O, -eps, GRV_D).cut(rrect_offset(GRV_I, -2 * eps, GRV_D + eps)))

# ---------------- interior pad behind the two back ports on the -X wall ----------------
PAD_Y_TOP = D - PORT_Y - 12.0   # free edge of the pad at the ceiling
PAD_Y_BOT = D - PORT_Y - 8.0    # free edge of the pad at the opening
pad_pts = [(PAD_Y_BOT, EDGE_CH), (CY1 + 0.5, EDGE_CH), (CY1 + 0.5, CAV_H + 0.5), (PAD_Y_TOP, CAV_H + 0.5)]
pad = cq.Workplane("YZ").workplane(offset=CX0 - 0.5).polyline(pad_pts).close().extrude(PAD_T + 0.5)
pad = pad.edges(
    cq.selectors.BoxSelector((CX0 + PAD_T - 0.1, PAD_Y_TOP - 0.5, EDGE_CH + 0.2), (CX0 + PAD_T + 0.1, PAD_Y_BOT + 0.5, CAV_H))
).fillet(PAD_FR)
body = body.union(pad)

# ---------------- small chamfered (tapped) hole in the ceiling ----------------
ceil_hole = (
    cq.Workplane("XY")
    .workplane(offset=CAV_H - 0.01)
    .center(CH_X, CH_Y)
    .circle(CH_CSK / 2)
    .workplane(offset=(CH_CSK - CH_D) / 2)
    .circle(CH_D / 2)
    .loft()
)
ceil_hole = ceil_hole.union(
    cq.Workplane("XY").workplane(offset=CAV_H - 0.01).center(CH_X, CH_Y).circle(CH_D / 2).extrude(CH_DEPTH)
)
body = body.cut(ceil_hole)


# ---------------- ports on the +X / -X faces ----------------
def xhole(x_face, y, z, dia, depth):
    d = -1 if x_face > 0 else 1
    wp = cq.Workplane("YZ").workplane(offset=x_face - d * eps)
    return wp.center(y, z).circle(dia / 2).extrude(d * (depth + eps))


# the front +X bore is run across the cavity up to the -X wall
body = body.cut(xhole(W, PORT_Y, PORT_ZP, BIG_T, W - WALL_XM + 0.3))
body = body.cut(xhole(W, D - PORT_Y, PORT_ZP, BIG_P, WALL_XP + CAV_R + 0.5))
body = body.cut(xhole(0, PORT_Y, PORT_ZM, BIG_T, WALL_XM + CAV_R + 0.5))
body = body.cut(xhole(0, D - PORT_Y, PORT_ZM, BIG_T, WALL_XM + PAD_T + 0.5))
body = body.cut(xhole(0, D - PORT_Y, LOW_Z, BIG_P, WALL_XM + PAD_T + 0.5))

# ---------------- small holes, same pattern on all four sides ----------------
for (cx, z) in [(0.0, SM_ZH), (-SM_DX, SM_ZL), (SM_DX, SM_ZL)]:
    # +X face (blind) / -X face (through)
    body = body.cut(xhole(W, D / 2 + cx, z, SM_D, SM_BLIND))
    body = body.cut(xhole(0, D / 2 - cx, z, SM_D, WALL_XM + 1.0))
    # -Y face (blind)
    fy = cq.Workplane("XZ").workplane(offset=eps).center(W / 2 + cx, z).circle(SM_D / 2).extrude(-(SM_BLIND + eps))
    body = body.cut(fy)
    # +Y face (through)
    by = cq.Workplane("XZ").workplane(offset=-(D + eps)).center(W / 2 - cx, z).circle(SM_D / 2).extrude(WALL_YP + 2 * eps)
    body = body.cut(by)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
